import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
H = 740.0            # overall height (Z)
W = 475.0            # overall width of sleeve/band and rib envelope (Y)
L_BOX = 426.0        # length of ribbed box (X)
L_BAND = 208.0       # length of wrapping band/sleeve (X)
RIB_D = 24.0         # rib protrusion from box wall
RIB_END_R = 12.0     # plan radius of rib ends
RIB_T = 10.0         # rib thickness
RIB_Z = [82.0, 217.0, 309.0, 433.0, 561.0, 653.0]
BOX_W = W - 2 * RIB_D
BOX_EDGE_R = 8.0
BAND_R = 40.0        # band profile corner radius
BAND_EDGE_R = 3.0    # sleeve edge radius at the head end
BAND_EDGE_R_IN = 10.0  # sleeve edge radius facing the ribbed box
CH_Y = [-60.0, -27.0, 30.0, 56.0]   # channel: top edge, floor, floor, top edge
CH_D = 25.0          # top channel depth
CH_RADII = [6.0, 12.0, 8.0, 6.0]   # +Y shoulder, +Y floor, -Y floor, -Y shoulder
DRAIN_R = 5.0
CH_END = 10.0        # channel stops this far short of the sleeve
FOLD_TOP = 2.0       # deg, cross-break fold on top panel
FOLD_BOT = 1.0       # deg, cross-break fold on bottom panel
FOLD_END = [0.25, 0.5, 0.75]   # deg, folds on the -X end panel
CREASE_TOP_Y = (193.0, 112.0)  # top crease: Y at x=0 and at x=L_BOX
CREASE_BOT_Y = -92.0           # bottom crease runs from (0,+Y edge) to (L_BOX, this Y)
CREASE_END_Z = [H, 623.0, 430.0]   # end-panel creases start on the +Y edge at these Z

# duct head on the +X face of the band
X0 = L_BOX + L_BAND
P_ZTOP = 658.0
P_ZBOT = 208.0
NOSE_DX = 188.0
NOSE_Y = -55.0
NOSE_R = 124.0
PLATE_T = 8.0
SHELL_T = 3.0
SHELL_GAP = 0.0      # shell runs this far inside the plate edge
BASE_INSET = 4.0
EMBED = 1.0          # fittings sink this far into the sleeve face
WEB_GAP = 0.3        # hairline clearance between fittings and shell skin
FL_W = 24.0          # flange strip width
FL_T = 10.0
GUSSET_Z = [557.0, 430.0, 306.0]
GUSSET_T = 2.5
GUSSET_LEN_M = 90.0  # web length on -Y flank
GUSSET_LEN_P = 32.0  # web length on +Y flank
TOP_HOLE_R = 72.0
TOP_BOLT_R = 97.0
TOP_BOLT_HOLE_R = 7.0
ROW_HOLE_Y = [28.0, -30.0, -88.0]   # row of small holes by the sleeve
ROW_HOLE_R = 4.5
ROW_HOLE_DX = 14.0   # row distance from the sleeve face
BOT_HOLE_R = 48.0
BOT_BOLT_R = 62.0
BOT_BOLT_HOLE_R = 7.5
SMALL_HOLE_R = 6.0
TAB_HOLE_R = 6.0
HOLE_DEPTH = 40.0
TAB_HOLE_Z = [624.0, 497.0, 372.0, 245.0]
END_HOLE_TOP = 14.0     # top hole in sleeve end face, below the top
END_HOLE_LOW_Z = 113.0  # lower pair of holes in sleeve end face
EDGE_HOLE_IN = 12.5     # hole centre distance from sleeve side


# ---------------------------------------------------------------- helpers
def tangent_point(p, c, r, side):
    """Tangent point on circle (c, r) seen from external point p."""
    dx, dy = p[0] - c[0], p[1] - c[1]
    d = math.hypot(dx, dy)
    a = math.atan2(dy, dx)
    b = math.acos(r / d)
    t = a + side * b
    return (c[0] + r * math.cos(t), c[1] + r * math.sin(t))


def nose_geometry():
    c = (X0 + NOSE_DX, NOSE_Y)
    pp = (X0 - EMBED, W / 2 - BASE_INSET)
    pm = (X0 - EMBED, -W / 2 + BASE_INSET)
    tp = tangent_point(pp, c, NOSE_R, -1)
    tm = tangent_point(pm, c, NOSE_R, +1)
    return c, pp, pm, tp, tm


def plate_outline():
    """Top/bottom plate: straight flanks tangent to the round nose."""
    c, pp, pm, tp, tm = nose_geometry()
    mid = (c[0] + NOSE_R, c[1])
    return (cq.Workplane("XY").moveTo(*pm)
            .lineTo(*tm).threePointArc(mid, tp).lineTo(*pp).close())


def _offset_line_pt(a, b, c, d, x):
    """Point at abscissa x on line a-b shifted by d towards point c."""
    dx, dy = b[0] - a[0], b[1] - a[1]
    L = math.hypot(dx, dy)
    ux, uy = dx / L, dy / L
    nx, ny = -uy, ux
    if (c[0] - a[0]) * nx + (c[1] - a[1]) * ny < 0:
        nx, ny = -nx, -ny
    a2 = (a[0] + nx * d, a[1] + ny * d)
    t = (x - a2[0]) / ux
    return (x, a2[1] + t * uy)


def shell_points(extra=0.0):
    """Through-points of the smooth shell curve: leaves the band face square,
    runs along the plate flanks and wraps round the nose."""
    c, pp, pm, tp, tm = nose_geometry()
    ap = math.atan2(tp[1] - c[1], tp[0] - c[0])
    am = math.atan2(tm[1] - c[1], tm[0] - c[0])
    d = SHELL_GAP + extra
    y0 = W / 2 - FL_W - extra
    pts = [(X0, -y0)]
    for x in (110.0, 170.0):
        pts.append(_offset_line_pt(pm, tm, c, d, X0 + x))
    n = 6
    for i in range(n + 1):
        t = am + (ap - am) * i / n
        pts.append((c[0] + (NOSE_R - d) * math.cos(t),
                    c[1] + (NOSE_R - d) * math.sin(t)))
    for x in (200.0, 150.0, 100.0, 60.0, 30.0):
        pts.append(_offset_line_pt(pp, tp, c, d, X0 + x))
    pts.append((X0, y0))
    return pts


def shell_wire(extra, z):
    """Closed wire at height z: one spline edge plus the chord on the band face."""
    p3 = [cq.Vector(x, y, z) for x, y in shell_points(extra)]
    sp = cq.Edge.makeSpline(p3, tangents=[cq.Vector(1, 0, 0), cq.Vector(-1, 0, 0)])
    return cq.Wire.assembleEdges([sp, cq.Edge.makeLine(p3[-1], p3[0])])


def shell_prism(extra, z0, z1):
    """Vertical prism on the shell curve (ruled loft keeps one clean side face)."""
    solid = cq.Solid.makeLoft([shell_wire(extra, z0), shell_wire(extra, z1)], True)
    return cq.Workplane("XY").add(solid)


def rounded_poly(wp, pts, radii):
    """Closed wire through pts with a tangent arc of radius radii[i]
    at each corner (0 = sharp)."""
    n = len(pts)
    segs = []
    for i in range(n):
        p = pts[i]
        a = pts[i - 1]
        b = pts[(i + 1) % n]
        r = radii[i]
        if r <= 0:
            segs.append((p, None, p))
            continue
        u1 = (a[0] - p[0], a[1] - p[1])
        u2 = (b[0] - p[0], b[1] - p[1])
        l1, l2 = math.hypot(*u1), math.hypot(*u2)
        u1 = (u1[0] / l1, u1[1] / l1)
        u2 = (u2[0] / l2, u2[1] / l2)
        cosang = max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1]))
        half = math.acos(cosang) / 2
        t = r / math.tan(half)
        t1 = (p[0] + u1[0] * t, p[1] + u1[1] * t)
        t2 = (p[0] + u2[0] * t, p[1] + u2[1] * t)
        bis = (u1[0] + u2[0], u1[1] + u2[1])
        lb = math.hypot(*bis)
        bis = (bis[0] / lb, bis[1] / lb)
        cd = r / math.sin(half)
        cc = (p[0] + bis[0] * cd, p[1] + bis[1] * cd)
        m = (cc[0] - bis[0] * r, cc[1] - bis[1] * r)
        segs.append((t1, m, t2))
    w = wp.moveTo(*segs[0][2])
    for i in range(1, n + 1):
        t1, m, t2 = segs[i % n]
        w = w.lineTo(*t1)
        if m is not None:
            w = w.threePointArc(m, t2)
    return w.close()


def halfspace(point, xdir, normal, size=4000.0):
    """Large box filling the half-space on the +normal side of a plane."""
    pl = cq.Plane(origin=point, xDir=xdir, normal=normal)
    return cq.Workplane(pl).rect(size, size).extrude(size / 2)


# ---------------------------------------------------------------- ribbed box
# cross-section (YZ) with the trapezoidal top channel, extruded along X
hw = BOX_W / 2
prof = [(-hw, 0.0), (hw, 0.0), (hw, H),
        (CH_Y[3], H), (CH_Y[2], H - CH_D), (CH_Y[1], H - CH_D), (CH_Y[0], H),
        (-hw, H)]
rads = [BOX_EDGE_R, BOX_EDGE_R, BOX_EDGE_R] + CH_RADII + [BOX_EDGE_R]
box = rounded_poly(cq.Workplane("YZ"), prof, rads).extrude(L_BOX)

# ribs on both long faces: round-nosed bars, ends rounded in plan at -X
for z in RIB_Z:
    for s in (1, -1):
        yc = s * (BOX_W / 2 + (RIB_D - 4) / 2)
        bar = (cq.Workplane("YZ")
               .center(yc, z)
               .slot2D(RIB_D + 4, RIB_T, 0)
               .extrude(L_BOX))
        plan = (cq.Workplane("XY", origin=(0, 0, z - RIB_T))
                .center(L_BOX / 2, yc)
                .rect(L_BOX, RIB_D + 4)
                .extrude(2 * RIB_T))
        plan = plan.edges("|Z").edges("<X").edges(">Y" if s > 0 else "<Y").fillet(RIB_END_R)
        box = box.union(bar.intersect(plan))

# channel stops short of the sleeve: plug the last CH_END mm, drain hole
plug = (cq.Workplane("XY")
        .box(CH_END, CH_Y[3] - CH_Y[0] + 30, CH_D + 6, centered=False)
        .translate((L_BOX - CH_END, CH_Y[0] - 15, H - CH_D - 6)))
box = box.union(plug)
drain = (cq.Workplane("YZ", origin=(L_BOX - CH_END - 1, 0, 0))
         .center(0.5 * (CH_Y[1] + CH_Y[2]), H - CH_D / 2)
         .circle(DRAIN_R).extrude(6))
box = box.cut(drain)


# cross-break folds (shallow sheet-metal creases) on top, bottom and end
# top panel, +Y side of the channel
p1 = cq.Vector(0, CREASE_TOP_Y[0], H)
p2 = cq.Vector(L_BOX, CREASE_TOP_Y[1], H)
d = (p2 - p1).normalized()
perp = cq.Vector(-d.y, d.x, 0)          # towards +Y side of the crease
if perp.y < 0:
    perp = perp * -1
t = math.tan(math.radians(FOLD_TOP))
n = (perp * t + cq.Vector(0, 0, 1)).normalized()
box = box.cut(halfspace(p1, d, n))

# bottom panel
p1 = cq.Vector(0, hw, 0)
p2 = cq.Vector(L_BOX, CREASE_BOT_Y, 0)
d = (p2 - p1).normalized()
perp = cq.Vector(-d.y, d.x, 0)
if perp.x < 0:
    perp = perp * -1
t = math.tan(math.radians(FOLD_BOT))
n = (perp * (-t) + cq.Vector(0, 0, 1)).normalized()
box = box.cut(halfspace(p1, d, n * -1))

# -X end panel: three parallel 45 deg creases (convex fold sequence)
q = cq.Vector(0, 1, -1).normalized()     # across the creases
dline = cq.Vector(0, -1, -1).normalized()
starts = [cq.Vector(0, hw, zc) for zc in CREASE_END_Z]
offs = [q.dot(p - starts[0]) for p in starts]
depth = 0.0
for k, p in enumerate(starts):
    if k > 0:
        depth += math.tan(math.radians(FOLD_END[k - 1])) * (offs[k] - offs[k - 1])
    sk = math.tan(math.radians(FOLD_END[k]))
    n = (cq.Vector(1, 0, 0) - q * sk).normalized()
    box = box.cut(halfspace(p + cq.Vector(depth, 0, 0), dline, n * -1))

# ---------------------------------------------------------------- band
band = (cq.Workplane("YZ", origin=(L_BOX, 0, 0))
        .center(0, H / 2)
        .rect(W, H)
        .extrude(L_BAND))
band = band.edges("|X").fillet(BAND_R)
band = band.faces("<X").edges().fillet(BAND_EDGE_R_IN)
band = band.faces(">X").edges().fillet(BAND_EDGE_R)

# holes in the +X end face of the band
endholes = (cq.Workplane("YZ", origin=(X0 + 1, 0, 0))
            .pushPoints([(0, H - END_HOLE_TOP), (W / 2 - EDGE_HOLE_IN, END_HOLE_LOW_Z),
                         (-W / 2 + EDGE_HOLE_IN, END_HOLE_LOW_Z)])
            .circle(SMALL_HOLE_R).extrude(-HOLE_DEPTH))
band = band.cut(endholes)

# ---------------------------------------------------------------- duct head
# hollow head: one smooth spline wall with integral top/bottom plates
shell = shell_prism(0.0, P_ZBOT, P_ZTOP)
inner = shell_prism(SHELL_T, P_ZBOT + PLATE_T, P_ZTOP - PLATE_T)
head = shell.cut(inner)


def web(z0, t):
    """Horizontal triangular web filling plate outline outside the shell
    near the band face (plate overhangs and gussets)."""
    g = plate_outline().extrude(t).translate((0, 0, z0))
    g = g.cut(shell_prism(-WEB_GAP, z0 - 1, z0 + t + 1))
    clip = (cq.Workplane("XY")
            .box(GUSSET_LEN_M, W, t + 4, centered=(False, False, False))
            .translate((X0 - 1, -W, z0 - 2))
            .union(cq.Workplane("XY")
                   .box(GUSSET_LEN_P, W, t + 4, centered=(False, False, False))
                   .translate((X0 - 1, 0, z0 - 2))))
    return g.intersect(clip)


# webs and flange strips are welded to the sleeve face; a hairline
# clearance to the shell keeps the shell skin one smooth face
fittings = web(P_ZTOP - PLATE_T, PLATE_T).union(web(P_ZBOT, PLATE_T))
for gz in GUSSET_Z:
    fittings = fittings.union(web(gz - GUSSET_T / 2, GUSSET_T))

# bolting flange strips on the band face, one per bay
levels = [P_ZTOP] + GUSSET_Z + [P_ZBOT]
gap = 3.0
tab_holes = []
for i in range(len(levels) - 1):
    z1, z0 = levels[i] - gap, levels[i + 1] + gap
    zc = 0.5 * (z0 + z1)
    for s in (1, -1):
        tw = FL_W - 1 - WEB_GAP
        yc = s * (W / 2 - 1 - tw / 2)
        tab = (cq.Workplane("XY")
               .box(FL_T + EMBED, tw, z1 - z0)
               .translate((X0 + (FL_T - EMBED) / 2, yc, zc)))
        hole = (cq.Workplane("YZ", origin=(X0 - 1, 0, 0))
                .center(s * (W / 2 - EDGE_HOLE_IN), TAB_HOLE_Z[i])
                .circle(TAB_HOLE_R).extrude(FL_T + 3))
        fittings = fittings.union(tab.cut(hole))
        tab_holes.append((s * (W / 2 - EDGE_HOLE_IN), TAB_HOLE_Z[i]))

# holes in top plate
c = (X0 + NOSE_DX, NOSE_Y)
top_cut = (cq.Workplane("XY", origin=(0, 0, P_ZTOP + 1))
           .center(*c).circle(TOP_HOLE_R).extrude(-PLATE_T - 2))
pts = [(c[0] + TOP_BOLT_R * math.cos(math.radians(30 + 60 * k)),
        c[1] + TOP_BOLT_R * math.sin(math.radians(30 + 60 * k))) for k in range(6)]
top_cut = top_cut.union(cq.Workplane("XY", origin=(0, 0, P_ZTOP + 1))
                        .pushPoints(pts).circle(TOP_BOLT_HOLE_R).extrude(-PLATE_T - 2))
top_cut = top_cut.union(cq.Workplane("XY", origin=(0, 0, P_ZTOP + 1))
                        .pushPoints([(X0 + ROW_HOLE_DX, y) for y in ROW_HOLE_Y])
                        .circle(ROW_HOLE_R).extrude(-PLATE_T - 2))
head = head.cut(top_cut)

# holes in bottom plate
bot_cut = (cq.Workplane("XY", origin=(0, 0, P_ZBOT - 1))
           .center(*c).circle(BOT_HOLE_R).extrude(PLATE_T + 2))
pts = [(c[0] + BOT_BOLT_R * math.cos(math.radians(60 * k)),
        c[1] + BOT_BOLT_R * math.sin(math.radians(60 * k))) for k in range(6)]
bot_cut = bot_cut.union(cq.Workplane("XY", origin=(0, 0, P_ZBOT - 1))
                        .pushPoints(pts).circle(BOT_BOLT_HOLE_R).extrude(PLATE_T + 2))
head = head.cut(bot_cut)

result = box.union(band).union(head).union(fittings)
# fastener holes continue into the sleeve end plate behind the flange strips
result = result.cut(cq.Workplane("YZ", origin=(X0 + 1, 0, 0))
                    .pushPoints(tab_holes).circle(TAB_HOLE_R).extrude(-HOLE_DEPTH))

VIEW = {"azimuth": 45, "elevation": 26}
